import math
import cadquery as cq

# ---------------------------------------------------------------- parameters
BASE = 18.0            # keycap footprint (square)
PITCH_X = 20.0         # nominal column pitch (see LAYOUT)
PITCH_Y = 20.35        # nominal row pitch (see LAYOUT)

# sculpted row profiles (row 0 = front row): rim height at front/back, front-wall inset
ROW_PROFILES = {
    0: dict(h_front=7.96, h_back=7.25, inset_front=3.1),
    1: dict(h_front=7.66, h_back=7.02, inset_front=3.65),
    2: dict(h_front=7.75, h_back=7.16, inset_front=3.95),
}
INSET_SIDE = 3.0       # side wall inset at the top
INSET_BACK = 0.3       # back wall inset at the top (near vertical back)
R_BASE = 1.8           # plan corner radius at the base
R_TOP = 1.1            # plan corner radius at the top
DISH_DEPTH = 1.0       # cylindrical dish depth
RIM_FILLET = 0.25

WALL = 1.2             # shell wall thickness
CEIL = 5.0             # height of the inner ceiling
STEM = 5.6             # square stem size
STEM_BOT = 0.8         # stem bottom height
CROSS_L, CROSS_W, CROSS_D = 4.1, 1.3, 3.8

ICON_TOP = 8.0         # flat top of the raised legends
ICON_BOT = 5.9         # legends are extruded from inside the top skin
CUT_Z0, CUT_Z1 = ICON_BOT - 1.0, ICON_TOP + 1.0   # through-cuts inside a legend

OW_R = 7.5             # overwatch drum radius
OW_RI = 5.4            # inner radius of the logo ring
OW_DY = 0.95           # drum centre offset towards the back
OW_TOP = 8.4
OW_RECESS = 1.2
OW_CAV_R = 5.3         # hollow inside the drum (seen from below)
OW_CAV_TOP = 6.2

ZL = 10.0              # loft height used to build the walls (cut afterwards)

VIEW = {"azimuth": 45, "elevation": 26}


# ---------------------------------------------------------------- helpers
def wall_rect(z, pr):
    """outer footprint (x0, x1, y0, y1) of the keycap walls at height z"""
    k = z / pr["h_front"]
    return (-BASE / 2 + INSET_SIDE * k, BASE / 2 - INSET_SIDE * k,
            -BASE / 2 + pr["inset_front"] * k, BASE / 2 - INSET_BACK * k)


def rrect_wire(x0, x1, y0, y1, r, z):
    r = min(r, (x1 - x0) / 2 - 1e-3, (y1 - y0) / 2 - 1e-3)
    wp = (cq.Workplane("XY").workplane(offset=z)
          .moveTo(x0 + r, y0).lineTo(x1 - r, y0)
          .radiusArc((x1, y0 + r), -r)
          .lineTo(x1, y1 - r)
          .radiusArc((x1 - r, y1), -r)
          .lineTo(x0 + r, y1)
          .radiusArc((x0, y1 - r), -r)
          .lineTo(x0, y0 + r)
          .radiusArc((x0 + r, y0), -r)
          .close())
    return wp.wires().val()


def r_at(z, pr):
    return R_BASE + (R_TOP - R_BASE) * z / pr["h_front"]


def loft_box(z0, z1, shrink, pr, dr=0.0):
    a = wall_rect(z0, pr)
    b = wall_rect(z1, pr)
    r0 = max(r_at(z0, pr) - dr, 0.4)
    r1 = max(r_at(z1, pr) - dr, 0.4)
    w0 = rrect_wire(a[0] + shrink, a[1] - shrink, a[2] + shrink, a[3] - shrink, r0, z0)
    w1 = rrect_wire(b[0] + shrink, b[1] - shrink, b[2] + shrink, b[3] - shrink, r1, z1)
    return cq.Solid.makeLoft([w0, w1], True)


def make_outer(pr):
    hf, hb = pr["h_front"], pr["h_back"]
    y_f = -BASE / 2 + pr["inset_front"]
    y_b = BASE / 2 - INSET_BACK
    tilt = math.atan2(hf - hb, y_b - y_f)
    half_w = BASE / 2 - INSET_SIDE
    dish_r = (half_w ** 2 + DISH_DEPTH ** 2) / (2 * DISH_DEPTH)

    body = cq.Workplane("XY").add(loft_box(0.0, ZL, 0.0, pr))
    # tilted top plane (kept just above the dish rim)
    big = 60.0
    cutter = (cq.Workplane("XY").box(big, big, big, centered=(True, True, False))
              .rotate((0, 0, 0), (1, 0, 0), -math.degrees(tilt))
              .translate((0, y_f, hf + 0.35)))
    body = body.cut(cutter)
    # cylindrical dish, axis parallel to the tilted rim, running front to back
    d = cq.Vector(0, math.cos(tilt), -math.sin(tilt))
    n = cq.Vector(0, math.sin(tilt), math.cos(tilt))
    p = cq.Vector(0, y_f, hf) + n * (dish_r - DISH_DEPTH) - d * 20
    dish = cq.Solid.makeCylinder(dish_r, 60, p, d)
    body = body.cut(cq.Workplane("XY").add(dish))
    try:
        body = body.faces("%CYLINDER").edges().fillet(RIM_FILLET)
    except Exception:
        pass
    return body


def make_cavity(pr):
    return cq.Workplane("XY").add(loft_box(-0.5, CEIL, WALL, pr, 0.4))


def make_stem(top=CEIL):
    stem = (cq.Workplane("XY").workplane(offset=STEM_BOT)
            .rect(STEM, STEM).extrude(top - STEM_BOT + 0.3)
            .edges("|Z").fillet(0.6))
    cross = (cq.Workplane("XY").workplane(offset=STEM_BOT - 0.5)
             .rect(CROSS_L, CROSS_W).extrude(CROSS_D + 0.5)
             .union(cq.Workplane("XY").workplane(offset=STEM_BOT - 0.5)
                    .rect(CROSS_W, CROSS_L).extrude(CROSS_D + 0.5)))
    return stem.cut(cross)


# ------------------------------------------------------------ 2D-ish legend helpers
def _wp(z0=ICON_BOT):
    return cq.Workplane("XY").workplane(offset=z0)


def poly(pts, z0=ICON_BOT, z1=ICON_TOP):
    return _wp(z0).polyline(pts).close().extrude(z1 - z0)


def circ(cx, cy, r, z0=ICON_BOT, z1=ICON_TOP):
    return _wp(z0).center(cx, cy).circle(r).extrude(z1 - z0)


def ring(cx, cy, ro, ri, z0=ICON_BOT, z1=ICON_TOP):
    return _wp(z0).center(cx, cy).circle(ro).circle(ri).extrude(z1 - z0)


def stroke(p1, p2, w, z0=ICON_BOT, z1=ICON_TOP):
    cx, cy = (p1[0] + p2[0]) / 2, (p1[1] + p2[1]) / 2
    L = math.hypot(p2[0] - p1[0], p2[1] - p1[1])
    ang = math.degrees(math.atan2(p2[1] - p1[1], p2[0] - p1[0]))
    return _wp(z0).center(cx, cy).slot2D(L + w, w, ang).extrude(z1 - z0)


def rbox(x0, x1, y0, y1, r=0.3, z0=ICON_BOT, z1=ICON_TOP):
    s = _wp(z0).center((x0 + x1) / 2, (y0 + y1) / 2).rect(x1 - x0, y1 - y0).extrude(z1 - z0)
    if r > 0:
        s = s.edges("|Z").fillet(r)
    return s


def half_disc(cx, cy, r, direction, z0=ICON_BOT, z1=ICON_TOP):
    """half disc with flat side through (cx, cy); direction 'right' or 'down' etc."""
    d = circ(cx, cy, r, z0, z1)
    if direction == "right":
        k = rbox(cx - r - 1, cx, cy - r - 1, cy + r + 1, 0, z0 - 1, z1 + 1)
    elif direction == "up":
        k = rbox(cx - r - 1, cx + r + 1, cy - r - 1, cy, 0, z0 - 1, z1 + 1)
    else:  # down
        k = rbox(cx - r - 1, cx + r + 1, cy, cy + r + 1, 0, z0 - 1, z1 + 1)
    return d.cut(k)


def U(*parts):
    s = parts[0]
    for p in parts[1:]:
        s = s.union(p)
    return s


# ------------------------------------------------------------ legends (key-local mm, +y = back)
def icon_steam():
    disc = circ(0.3, 1.1, 5.35)
    wedge = poly([(-6.0, 1.2), (-3.4, -0.6), (-6.0, -2.2)], CUT_Z0, CUT_Z1)
    rod = stroke((-3.9, -1.0), (1.6, 2.9), 1.3, CUT_Z0, CUT_Z1)
    wheel = ring(1.6, 2.9, 1.8, 0.9, CUT_Z0, CUT_Z1)
    return disc.cut(wedge).cut(rod).cut(wheel)


def icon_code():
    w = 1.05
    return U(stroke((-5.07, 1.57), (-2.78, 3.49), w),
             stroke((-5.07, 1.57), (-2.78, -0.34), w),
             stroke((1.05, 4.83), (-1.05, -1.88), w),
             stroke((5.27, 1.57), (2.78, 3.49), w),
             stroke((5.27, 1.57), (2.78, -0.34), w))


def icon_pickaxe():
    return U(stroke((-4.6, -3.2), (2.6, 4.6), 1.0),
             stroke((-1.8, 5.35), (2.8, 5.35), 1.15),
             poly([(2.3, 5.9), (3.9, 5.9), (4.4, 4.6), (3.4, 3.8), (2.3, 4.5)]),
             stroke((4.0, 4.4), (4.25, -0.45), 1.15))


def icon_vol_low():
    spk = poly([(-4.4, 3.3), (-1.7, 3.3), (1.15, 6.3), (1.15, -3.0), (-1.7, -0.55), (-4.4, -0.55)])
    return spk.union(half_disc(2.9, 1.67, 1.45, "right"))


def icon_vol():
    spk = poly([(-4.95, 2.9), (-2.45, 2.9), (0.05, 5.6), (0.05, -3.2), (-2.45, -0.73), (-4.95, -0.73)])
    return spk.union(half_disc(1.6, 1.28, 3.7, "right"))


def icon_camera():
    outer = U(rbox(-4.7, 4.7, -2.25, 4.45, 0.7),
              poly([(-1.8, 4.0), (-1.3, 5.8), (1.7, 5.8), (2.2, 4.0)]))
    inner = U(rbox(-3.5, 3.5, -0.95, 3.15, 0.3, CUT_Z0, CUT_Z1),
              poly([(-1.0, 3.0), (-0.7, 4.75), (1.1, 4.75), (1.4, 3.0)], CUT_Z0, CUT_Z1))
    return outer.cut(inner).union(ring(0.0, 1.35, 2.2, 1.3))


def icon_playpause():
    return U(poly([(-4.5, 4.2), (-4.5, -1.1), (-0.45, 1.55)]),
             rbox(-0.05, 1.65, -1.1, 4.15, 0.3),
             rbox(2.85, 4.65, -1.1, 4.15, 0.3))


def icon_discord():
    ox = -0.15
    P = lambda x, y: (x + ox, y)
    body = (_wp().moveTo(*P(-2.0, 4.95))
            .threePointArc(P(0.0, 4.4), P(2.0, 4.95))
            .threePointArc(P(4.55, 2.6), P(5.0, -0.9))
            .threePointArc(P(4.3, -2.25), P(3.0, -2.85))
            .lineTo(*P(2.3, -1.9))
            .threePointArc(P(0.0, -2.35), P(-2.3, -1.9))
            .lineTo(*P(-3.0, -2.85))
            .threePointArc(P(-4.3, -2.25), P(-5.0, -0.9))
            .threePointArc(P(-4.55, 2.6), P(-2.0, 4.95))
            .close().extrude(ICON_TOP - ICON_BOT))
    eyes = U(circ(ox - 1.6, 0.6, 1.0, CUT_Z0, CUT_Z1),
             circ(ox + 1.6, 0.6, 1.0, CUT_Z0, CUT_Z1))
    return body.cut(eyes)


def circle_segment(cx, cy, r, p0, p1, offset, z0=ICON_BOT, z1=ICON_TOP):
    """part of the circle on the left-hand side of the line p0->p1, shifted by offset"""
    ux, uy = p1[0] - p0[0], p1[1] - p0[1]
    L = math.hypot(ux, uy)
    ux, uy = ux / L, uy / L
    nx, ny = -uy, ux
    qx, qy = p0[0] + nx * offset, p0[1] + ny * offset
    # solve |q + t u - c|^2 = r^2
    dx, dy = qx - cx, qy - cy
    b = dx * ux + dy * uy
    cc = dx * dx + dy * dy - r * r
    disc = math.sqrt(b * b - cc)
    t1, t2 = -b - disc, -b + disc
    a1 = (qx + t1 * ux, qy + t1 * uy)
    a2 = (qx + t2 * ux, qy + t2 * uy)
    m = (cx + nx * r, cy + ny * r)
    return (_wp(z0).moveTo(*a1).lineTo(*a2).threePointArc(m, a1).close().extrude(z1 - z0))


def icon_speed_off():
    p0, p1 = (-4.3, -2.6), (4.6, 6.2)
    dial = circle_segment(-0.84, 1.76, 3.85, p0, p1, 0.2)
    hole = circle_segment(-0.84, 1.76, 2.85, p0, p1, 1.3, CUT_Z0, CUT_Z1)
    drop = stroke((2.85, -0.75), (2.85, 1.95), 3.2)
    slash = stroke(p0, p1, 0.9)
    return dial.cut(hole).union(drop).union(slash)


def icon_mic_off():
    caps = stroke((0.3, 0.8), (0.3, 5.0), 3.2)
    holder = ring(0.2, 1.75, 3.85, 3.1).cut(rbox(-5, 5, 1.75, 8, 0, CUT_Z0, CUT_Z1))
    stem = rbox(-0.25, 0.65, -3.9, -1.9, 0.2)
    slash = stroke((-3.6, -2.1), (3.85, 4.85), 0.75)
    return U(caps, holder, stem, slash)


def icon_monitor():
    frame = rbox(-3.85, 4.4, -0.35, 5.2, 0.6).cut(
        rbox(-2.85, 3.4, 0.45, 4.4, 0.3, CUT_Z0, CUT_Z1))
    return U(frame,
             rbox(-0.05, 0.65, -1.9, -0.2, 0),
             rbox(-2.3, 2.7, -2.85, -1.7, 0.5))


def make_overwatch_drum():
    cy = OW_DY
    drum = cq.Workplane("XY").workplane(offset=3.0).center(0, cy).circle(OW_R).extrude(OW_TOP - 3.0)
    recess = (cq.Workplane("XY").workplane(offset=OW_TOP - OW_RECESS).center(0, cy)
              .circle(OW_RI).extrude(OW_RECESS + 1))
    drum = drum.cut(recess)
    z0, z1 = OW_TOP - OW_RECESS - 0.2, OW_TOP

    def leg(sx):
        pts = [(sx * 0.25, 3.75), (sx * 1.9, 0.9), (sx * 5.5, -2.2), (sx * 3.3, -4.5), (sx * 0.25, -1.4)]
        pts = [(x, y + cy) for (x, y) in pts]
        p = (cq.Workplane("XY").workplane(offset=z0)
             .moveTo(*pts[0]).threePointArc(pts[1], pts[2]).lineTo(*pts[3]).lineTo(*pts[4]).close()
             .extrude(z1 - z0))
        return p
    drum = drum.union(leg(-1)).union(leg(1))
    for ang in (51.0, 129.0):
        a = math.radians(ang)
        cx, cyy = 6.6 * math.cos(a), cy + 6.6 * math.sin(a)
        gap = (cq.Workplane("XY").workplane(offset=OW_TOP - OW_RECESS)
               .center(cx, cyy).rect(3.0, 0.6).extrude(OW_RECESS + 1)
               .rotate((cx, cyy, 0), (cx, cyy, 1), ang))
        drum = drum.cut(gap)
    return drum


# ---------------------------------------------------------------- build
stem = make_stem()
bodies = {}
outers = {}
for row, pr in ROW_PROFILES.items():
    outers[row] = make_outer(pr)
    bodies[row] = outers[row].cut(make_cavity(pr)).union(stem)

# the overwatch cap is also hollowed up into its drum
ow_cavity = make_cavity(ROW_PROFILES[2]).union(
    cq.Workplane("XY").workplane(offset=-0.5).center(0, OW_DY).circle(OW_CAV_R).extrude(OW_CAV_TOP + 0.5))
ow_body = (outers[2].union(make_overwatch_drum())
           .cut(ow_cavity).union(make_stem(OW_CAV_TOP)))

# key -> (legend builder, column, row, dx, dy); row 0 is the front row.
# The caps sit on a PITCH_X x PITCH_Y grid but are hand placed, hence the small offsets.
LAYOUT = [
    (None,            0, 2, -0.10,  0.00),   # overwatch (raised drum logo)
    (icon_steam,      1, 2, -0.45,  0.00),
    (icon_code,       2, 2, -0.65, -0.05),
    (icon_pickaxe,    3, 2, -0.10, -0.10),
    (icon_vol_low,    0, 1,  0.10, -0.10),
    (icon_vol,        1, 1, -0.30, -0.10),
    (icon_camera,     2, 1,  0.20,  0.00),
    (icon_playpause,  3, 1,  0.05,  0.00),
    (icon_discord,    0, 0,  0.25,  0.00),
    (icon_speed_off,  1, 0,  0.50,  0.00),
    (icon_mic_off,    2, 0,  0.20,  0.00),
    (icon_monitor,    3, 0, -0.05,  0.15),
]

solids = []
for fn, col, row, dx, dy in LAYOUT:
    k = ow_body if fn is None else bodies[row].union(fn())
    k = k.translate(((col - 1.5) * PITCH_X + dx, (row - 1) * PITCH_Y + dy, 0))
    solids.extend(k.solids().vals())

result = cq.Workplane("XY").newObject([cq.Compound.makeCompound(solids)])
